import math

import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
# bottom socket sleeve
SLEEVE_D = 13.7
SLEEVE_H = 18.6
SLEEVE_BORE_D = 11.6
SLEEVE_BORE_DEPTH = 6.0
# thin ring flange on top of the sleeve
RING_D = 15.8
RING_T = 0.9
# tapered pole
POLE_D_BOT = 12.0
POLE_D_TOP = 8.2
POLE_LEN = 195.8
# collar under the head (D-shaped: rounded toward +X)
COLLAR_XMIN = -9.6
COLLAR_XMAX = 5.2
COLLAR_W = 9.7       # along Y
COLLAR_H = 6.2
COLLAR_R = 0.5       # fillet on the two -X corners of the collar
# head box
BOX_L = 27.5         # along X (at the bottom)
BOX_H = 15.8         # along Z
BOX_LEAN_X = 1.05    # +X end face leans back by this much over the height
BOX_W_BOT = 14.1     # along Y at the bottom
BOX_W_MID = 14.7     # along Y at mid height (side faces are crowned)
BOX_W_TOP = 13.1     # along Y at the top
BOX_R_BACK = 1.8     # corner fillet at the -X end
BOX_R_FRONT = 0.8    # corner fillet at the +X end
BOX_R_TOP = 0.4      # top perimeter fillet
NECK_R = 0.6         # fillet where the pole meets the collar
# clamping screw on the +X face, sitting in a shallow counterbore
CBORE_D = 3.6
CBORE_DEPTH = 0.7
CBORE_CHAMFER = 0.3
SCREW_D = 3.0
SCREW_PROUD = 0.3    # head top above the face centre
SLOT_W = 0.5
SLOT_DEPTH = 0.5
SLOT_ANGLE = 60.0    # slot direction on the face, degrees from +Y toward +Z

# ---------------- derived z-levels ----------------
z_ring = SLEEVE_H
z_pole = z_ring + RING_T
z_collar = z_pole + POLE_LEN
z_box = z_collar + COLLAR_H
z_top = z_box + BOX_H
z_mid = (z_box + z_top) / 2

# sleeve with bore from below
sleeve = cq.Workplane("XY").circle(SLEEVE_D / 2).extrude(SLEEVE_H)
sleeve = sleeve.cut(
    cq.Workplane("XY").circle(SLEEVE_BORE_D / 2).extrude(SLEEVE_BORE_DEPTH)
)

ring = cq.Workplane("XY").workplane(offset=z_ring).circle(RING_D / 2).extrude(RING_T)

# tapered pole (revolved trapezoid)
pole = (
    cq.Workplane("XZ")
    .polyline(
        [
            (0, z_pole),
            (POLE_D_BOT / 2, z_pole),
            (POLE_D_TOP / 2, z_collar),
            (0, z_collar),
        ]
    )
    .close()
    .revolve(360, (0, 0, 0), (0, 1, 0))
)

# collar: rectangle at -X end, semicircular at +X end
cr = COLLAR_W / 2
cx_arc = COLLAR_XMAX - cr
collar = (
    cq.Workplane("XY")
    .workplane(offset=z_collar)
    .moveTo(COLLAR_XMIN, -cr)
    .lineTo(cx_arc, -cr)
    .threePointArc((COLLAR_XMAX, 0), (cx_arc, cr))
    .lineTo(COLLAR_XMIN, cr)
    .close()
    .extrude(COLLAR_H)
)
collar = collar.edges("|Z and <X").fillet(COLLAR_R)

# head box = front profile (XZ, leaning +X end)  intersected with
#            side profile (YZ, crowned side faces)
hx = BOX_L / 2
front = (
    cq.Workplane("XZ")
    .polyline(
        [
            (-hx, z_box),
            (hx, z_box),
            (hx - BOX_LEAN_X, z_top),
            (-hx, z_top),
        ]
    )
    .close()
    .extrude(BOX_W_MID, both=True)
)
yb, ym, yt = BOX_W_BOT / 2, BOX_W_MID / 2, BOX_W_TOP / 2
side = (
    cq.Workplane("YZ")
    .moveTo(-yb, z_box)
    .lineTo(yb, z_box)
    .threePointArc((ym, z_mid), (yt, z_top))
    .lineTo(-yt, z_top)
    .threePointArc((-ym, z_mid), (-yb, z_box))
    .close()
    .extrude(BOX_L, both=True)
)
box = front.intersect(side)


def _corner_edges(shape, back):
    """corner edges of the head running mostly along Z, at the -X (back) or +X end"""
    out = []
    for e in shape.Edges():
        p0, p1 = e.startPoint(), e.endPoint()
        c = e.Center()
        if abs(p1.z - p0.z) > 0.5 * BOX_H and abs(c.y) > 3.0:
            if (c.x < 0) == back:
                out.append(e)
    return out


bs = box.val()
bs = bs.fillet(BOX_R_BACK, _corner_edges(bs, True))
bs = bs.fillet(BOX_R_FRONT, _corner_edges(bs, False))
box = cq.Workplane("XY").add(bs)
box = box.faces(">Z").edges().fillet(BOX_R_TOP)

# counterbore + slotted screw on the +X face; their axis is normal to the leaning face
zc = z_mid
x_face = hx - BOX_LEAN_X / 2           # face position at mid height
lean_deg = math.degrees(math.atan2(BOX_LEAN_X, BOX_H))


def _on_face(wp):
    """move a feature built along +X at the origin onto the +X face"""
    return wp.rotate((0, 0, 0), (0, 1, 0), -lean_deg).translate((x_face, 0, zc))


cbore = _on_face(
    cq.Workplane("YZ")
    .workplane(offset=-CBORE_DEPTH)
    .circle(CBORE_D / 2)
    .extrude(CBORE_DEPTH + 2.0)
)
box = box.cut(cbore)
box = box.edges(
    cq.selectors.NearestToPointSelector((x_face, 0, zc + CBORE_D / 2))
).chamfer(CBORE_CHAMFER)

screw = (
    cq.Workplane("YZ")
    .workplane(offset=-CBORE_DEPTH - 0.1)
    .circle(SCREW_D / 2)
    .extrude(CBORE_DEPTH + 0.1 + SCREW_PROUD)
    .faces(">X")
    .edges()
    .chamfer(0.2)
)
slot = (
    cq.Workplane("YZ")
    .workplane(offset=SCREW_PROUD - SLOT_DEPTH)
    .transformed(rotate=(0, 0, SLOT_ANGLE))
    .rect(SCREW_D * 1.3, SLOT_W)
    .extrude(SLOT_DEPTH + 0.1)
)
screw = _on_face(screw.cut(slot))

# turn the round parts so their surface seams sit on the +Y side
SEAM_TURN = 90.0
sleeve = sleeve.rotate((0, 0, 0), (0, 0, 1), SEAM_TURN)
ring = ring.rotate((0, 0, 0), (0, 0, 1), SEAM_TURN)
pole = pole.rotate((0, 0, 0), (0, 0, 1), SEAM_TURN)

body = sleeve.union(ring).union(pole).union(collar)


def _neck_edges(shape):
    """the circular edge where the pole top meets the collar underside"""
    out = []
    for e in shape.Edges():
        c = e.Center()
        bb = e.BoundingBox()
        if (
            abs(bb.zmin - z_collar) < 1e-3
            and abs(bb.zmax - z_collar) < 1e-3
            and abs(bb.xlen - POLE_D_TOP) < 0.05
        ):
            out.append(e)
    return out


bsh = body.val()
bsh = bsh.fillet(NECK_R, _neck_edges(bsh))
body = cq.Workplane("XY").add(bsh)

result = body.union(box).union(screw)

VIEW = {"azimuth": 45, "elevation": 26}
